import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# oval plinth (tapered, elliptical)
BASE_H = 12.7
BASE_BOT_A, BASE_BOT_B = 33.0, 60.0      # semi-axes X, Y at bottom
BASE_TOP_A, BASE_TOP_B = 29.0, 52.5      # semi-axes X, Y at top

# head (face looks toward +X, head sits a little toward -Y)
HEAD_SECTIONS = [  # (z, x_back, x_front, y_right, y_left, corner r) rounded sections, neck to temples
    (20.0, -8.5, 19.0, -18.5, 8.5, 12.0),     # neck (hidden in the collar)
    (33.0, -13.0, 29.2, -18.5, 8.5, 12.0),    # chin
    (42.0, -19.5, 29.5, -22.5, 12.5, 15.5),   # mouth / jaw
    (55.0, -22.6, 26.4, -26.9, 14.3, 18.5),   # cheekbones / ears
    (66.0, -21.3, 23.3, -25.5, 12.9, 17.0),   # temples
]
# smooth spherical back of the head (behind the left ear)
BACK_BALL_C, BACK_BALL_R = (-7.0, -9.5, 59.0), 16.0
# crown: a second short loft from the temple section to a rounded top
CROWN_SECTIONS = [
    HEAD_SECTIONS[-1],
    (72.5, -19.1, 19.9, -21.8, 10.2, 14.0),
    (77.5, -13.5, 15.0, -18.5, 6.0, 11.0),
    (81.5, -8.0, 10.0, -13.5, 1.0, 6.5),
]
# the top of the crown is rounded off by a flat, wide dome
DOME_C, DOME_R = (0.5, -6.0, 58.0), (38.0, 33.0, 22.6)

NOSE_FILLET = 1.2
NOSE_Y = -4.0                             # nose centre line
EAR_X, EAR_Z = 4.0, 48.0
EAR_Y = (-25.5, 14.0)
EAR_R = (6.0, 3.0, 7.5)

# neck
NECK_C, NECK_R = (6.0, -5.0), (13.5, 14.0)

# back post that carries the head
POST_C = (-11.0, -4.0)
POST_R = 7.0
POST_TOP = 48.0

# torso shell
SHELL_T = 3.0
GAP_FRONT = -3.0
CHEST_BACK = -14.0
CHEST = [  # (z, cx, cy, a, b) ellipse sections of chest and collar
    (10.0, 1.5, -4.5, 23.5, 26.0),
    (22.0, 1.5, -4.5, 21.0, 22.5),
    (30.0, 1.0, -4.5, 18.0, 19.5),
    (38.0, 0.5, -4.5, 12.0, 16.0),
]
GAP_HALF_Y = 15.0
# shoulder cross-sections: (z, x_back, x_front, outer |y|, corner radius)
SHOULDER = [
    (10.0, -21.5, 18.5, 47.8, 10.0),
    (14.0, -21.5, 17.5, 46.8, 10.0),
    (17.5, -21.0, 15.5, 43.0, 9.0),
    (21.0, -19.5, 12.0, 36.0, 8.0),
    (23.0, -16.0, 7.0, 29.5, 6.0),
    (24.0, -11.0, 1.0, 26.0, 4.0),
]
SHOULDER_INNER = {1: 11.0, -1: -19.0}   # y of the inner (neck side) edge of each shoulder

VIEW = {"azimuth": 45, "elevation": 26}


def ellipsoid(c, r):
    """Triaxial ellipsoid made by scaling a unit sphere."""
    s = cq.Solid.makeSphere(1.0, angleDegrees1=-90, angleDegrees2=90)
    m = cq.Matrix([[r[0], 0, 0, 0], [0, r[1], 0, 0], [0, 0, r[2], 0]])
    s = s.transformGeometry(m)
    return cq.Workplane("XY").add(s.translate(cq.Vector(*c)))


def xz_profile(pts, y0, y1):
    """Closed spline profile in the XZ plane, extruded from y0 to y1."""
    wp = cq.Workplane("XZ", origin=(0, y1, 0))
    return wp.spline(pts, periodic=True).close().extrude(y1 - y0)


def rrect_loft(sections):
    """Smooth loft through rounded rectangles given as (z, x0, x1, y0, y1, r)."""
    sk = []
    for (z, x0, x1, y0, y1, r) in sections:
        r = min(r, 0.45 * min(x1 - x0, y1 - y0))
        s = cq.Sketch().rect(x1 - x0, y1 - y0).vertices().fillet(r)
        sk.append(s.moved(cq.Location(cq.Vector((x0 + x1) / 2.0, (y0 + y1) / 2.0, z))))
    return cq.Workplane("XY").placeSketch(*sk).loft()


def ellipse_loft(sections):
    """Smooth loft through ellipses given as (z, cx, cy, a, b)."""
    wp = cq.Workplane("XY")
    z_prev = 0.0
    for i, (z, cx, cy, a, b) in enumerate(sections):
        wp = wp.workplane(offset=z - z_prev) if i else wp.workplane(offset=z)
        wp = wp.center(cx, cy).ellipse(a, b).center(-cx, -cy)
        z_prev = z
    return wp.loft()


# ---------------- base ----------------
base = (
    cq.Workplane("XY")
    .ellipse(BASE_BOT_A, BASE_BOT_B)
    .workplane(offset=BASE_H)
    .ellipse(BASE_TOP_A, BASE_TOP_B)
    .loft(combine=True)
)

# ---------------- head: smooth loft from the neck to the temples, domed crown, trimmed to the profile ----------------
head_side = [  # (X, Z) silhouette seen from -Y
    (-6.0, 81.2), (8.0, 80.4), (17.5, 75.4), (23.2, 65.5), (25.0, 58.5),
    (25.0, 53.0), (27.0, 47.0), (29.0, 40.0), (28.7, 33.5), (26.0, 30.2),
    (21.0, 28.4), (19.6, 24.5), (19.0, 18.0), (6.0, 16.5), (-6.5, 18.0),
    (-7.0, 30.0), (-9.0, 40.0), (-15.0, 46.5), (-20.5, 50.5), (-22.6, 55.5),
    (-22.8, 61.0), (-21.0, 69.5), (-16.5, 76.2),
]
head_loft = rrect_loft(HEAD_SECTIONS)
crown = rrect_loft(CROWN_SECTIONS)
back_ball = cq.Workplane("XY").sphere(BACK_BALL_R).translate(BACK_BALL_C)
dome = ellipsoid(DOME_C, DOME_R).union(
    cq.Workplane("XY").box(100, 100, DOME_C[2], centered=(True, True, False))
)
head = (
    head_loft.union(crown).union(back_ball)
    .intersect(xz_profile(head_side, -40, 30))
    .intersect(dome)
)

# nose: wedge seen from the side, tapered seen from the front
nose_side = (
    cq.Workplane("XZ", origin=(0, 5.0, 0))
    .polyline([(22.0, 59.0), (34.2, 48.3), (33.2, 46.4), (29.0, 45.6), (22.0, 45.8)])
    .close()
    .extrude(20.0)
)
nose_front = (
    cq.Workplane("YZ", origin=(15.0, 0, 0))
    .polyline([(NOSE_Y - 3.0, 59.5), (NOSE_Y + 3.0, 59.5), (NOSE_Y + 5.5, 45.3), (NOSE_Y - 5.5, 45.3)])
    .close()
    .extrude(25.0)
)
nose = nose_side.intersect(nose_front)
try:
    nose = nose.edges().fillet(NOSE_FILLET)
except Exception:
    pass


def ear(y, side):
    """Flattened ear with a shallow bowl pressed into its outer face."""
    shell_ = ellipsoid((EAR_X, y, EAR_Z), EAR_R)
    bowl = ellipsoid((EAR_X + 0.8, y + side * EAR_R[1] * 0.9, EAR_Z + 0.5),
                     (EAR_R[0] * 0.62, EAR_R[1] * 0.6, EAR_R[2] * 0.62))
    return shell_.cut(bowl)


ears = ear(EAR_Y[0], -1).union(ear(EAR_Y[1], 1))

# ---------------- neck ----------------
neck = (
    cq.Workplane("XY", origin=(0, 0, BASE_H - 0.5))
    .center(*NECK_C)
    .ellipse(*NECK_R)
    .extrude(42.0 - BASE_H)
)

# ---------------- torso: two shoulder pads + chest/collar, shells open at the back ----------------


def shoulder(side, inset=0.0, back_open=False):
    secs = []
    for (z, xb, xf, yo, r) in SHOULDER:
        yi = SHOULDER_INNER[side] - side * (6.0 if back_open else 0.0)
        yo = side * yo - side * inset
        xb2 = -40.0 if back_open else xb
        y0, y1 = (yi, yo) if side > 0 else (yo, yi)
        secs.append((z - inset, xb2, xf - inset, y0, y1, max(r - inset, 1.0)))
    return rrect_loft(secs)


chest = ellipse_loft(CHEST).intersect(
    cq.Workplane("XY").box(60, 100, 60, centered=(False, True, False)).translate((CHEST_BACK, 0, 0))
)
torso = shoulder(1).union(shoulder(-1)).union(chest)
torso = torso.cut(shoulder(1, SHELL_T, True)).cut(shoulder(-1, SHELL_T, True))
# nothing behind the neck: the post stands free between the shoulder shells
back_gap = (
    cq.Workplane("XY", origin=(0, 0, 5.0))
    .center(-20.0 + GAP_FRONT / 2.0, POST_C[1])
    .rect(40.0 + GAP_FRONT, 2 * GAP_HALF_Y)
    .extrude(60)
)
torso = torso.cut(back_gap)

# ---------------- back post ----------------
post = (
    cq.Workplane("XY", origin=(0, 0, BASE_H - 0.5))
    .center(*POST_C)
    .circle(POST_R)
    .extrude(POST_TOP - BASE_H)
)

result = base.union(torso).union(neck).union(head).union(nose).union(ears).union(post)
